import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BX, BY, BH = 80.0, 75.9, 32.8      # enclosure outer size
R_OUT = 5.0                        # vertical corner radius (outside)
T_WALL = 2.4                       # wall thickness
T_FLOOR = 2.5                      # floor thickness
R_BOT = 3.6                        # bottom outer edge fillet
R_IN_BOT = 1.6                     # inner floor/wall fillet

# corner screw columns (3 corners, none at front-right)
# hole centre insets (x, y) from the outer faces: back-left, back-right, front-left
COL_INSETS = [(3.0, 4.7), (3.2, 4.7), (3.9, 3.9)]
COL_R = 2.4
COL_HOLE_D = 2.2
COL_CB_D, COL_CB_H = 3.8, 0.6

# notch in the +X wall
NOTCH_Y0, NOTCH_Y1 = -20.5, -7.0
NOTCH_DEPTH = 12.7

# PCB standoffs
SO_D, SO_HOLE_D, SO_TOP = 8.0, 2.5, 17.6
SO_PTS = [(-16.2, -3.6), (31.0, -3.6), (-16.2, -27.25), (31.0, -27.25)]

# small floor through holes
FH_D = 2.6
FH_PTS = [(-28.7, 14.5), (27.1, 14.5), (-28.3, -20.4), (27.4, -20.4)]

# cable tie bridges
BR_Y0, BR_Y1 = -16.25, -10.7
BR_X = [(-1.7, 10.1), (11.2, 23.5)]
BR_H = 10.8
BR_TUN_W, BR_TUN_H = 8.0, 6.5

# slotted post
UP_X0, UP_X1 = -35.3, -22.9
UP_Y0, UP_Y1 = 18.6, 25.3
UP_TOP = 21.4
UP_SLOT_W, UP_SLOT_D = 5.3, 11.0

# front panel
PN_W, PN_T = 59.2, 3.4
PN_Z0, PN_Z1 = 1.25, 46.55
PN_R = 3.5
PN_EDGE = 0.6
PN_HOLE_D = 3.0
PN_HOLES = [(-25.8, 42.0), (23.2, 42.0), (-25.8, 7.5), (23.2, 7.5)]
PN_WIN = (-28.6, -23.4, 19.6, 27.0)   # x0, x1, z0, z1
WALL_WIN = (-26.4, -23.4, 20.6, 27.0)  # smaller opening in the front wall behind it

# lid (placed beside the enclosure)
LID_CX, LID_CY, LID_Z0 = 118.3, -5.15, 0.0
LX, LY, LH = 80.45, 76.6, 3.8
L_FIL = 3.7
L_T = 1.2
L_WIN_W, L_WIN_H = 26.4, 13.8
L_WIN_DX, L_WIN_DY = -3.0, -15.5
L_HOLE_D = 3.1
L_COLLAR = 1.2                    # window collar depth below the lid skin


def rrect(w, h, r, z0, height):
    return (cq.Workplane("XY").workplane(offset=z0)
            .rect(w, h).extrude(height)
            .edges("|Z").fillet(r))


# ---------------- enclosure ----------------
box = rrect(BX, BY, R_OUT, 0, BH)
box = box.edges("<Z").fillet(R_BOT)

def corner_pts(w, h):
    (ax, ay), (bx, by), (cx, cy) = COL_INSETS
    return [(-w / 2 + ax, h / 2 - ay), (w / 2 - bx, h / 2 - by), (-w / 2 + cx, -h / 2 + cy)]


col_pts = corner_pts(BX, BY)
cav = rrect(BX - 2 * T_WALL, BY - 2 * T_WALL, R_OUT - T_WALL + 0.5, T_FLOOR, BH + 1)
cav = cav.edges("<Z").fillet(R_IN_BOT)
cols = (cq.Workplane("XY").workplane(offset=T_FLOOR - 1)
        .pushPoints(col_pts).circle(COL_R).extrude(BH + 3))
cav = cav.cut(cols)
box = box.cut(cav)

col_holes = (cq.Workplane("XY").workplane(offset=BH - 14)
             .pushPoints(col_pts).circle(COL_HOLE_D / 2).extrude(14.1))
box = box.cut(col_holes)
col_cb = (cq.Workplane("XY").workplane(offset=BH - COL_CB_H)
          .pushPoints(col_pts).circle(COL_CB_D / 2).extrude(COL_CB_H + 0.1))
box = box.cut(col_cb)

# notch in +X wall
notch = (cq.Workplane("XY")
         .box(T_WALL + 4, NOTCH_Y1 - NOTCH_Y0, NOTCH_DEPTH + 1, centered=False)
         .translate((BX / 2 - T_WALL - 2, NOTCH_Y0, BH - NOTCH_DEPTH)))
box = box.cut(notch)

# standoffs
so = (cq.Workplane("XY").workplane(offset=T_FLOOR - 0.1)
      .pushPoints(SO_PTS).circle(SO_D / 2).extrude(SO_TOP - T_FLOOR + 0.1))
box = box.union(so)
so_h = (cq.Workplane("XY").workplane(offset=T_FLOOR + 1.0)
        .pushPoints(SO_PTS).circle(SO_HOLE_D / 2).extrude(SO_TOP))
box = box.cut(so_h)

# floor holes
fh = (cq.Workplane("XY").workplane(offset=-1)
      .pushPoints(FH_PTS).circle(FH_D / 2).extrude(T_FLOOR + 2))
box = box.cut(fh)

# cable tie bridge (high-X block, tunnel along Y) and plain block beside it
for i, (x0, x1) in enumerate(BR_X):
    blk = (cq.Workplane("XY").box(x1 - x0, BR_Y1 - BR_Y0, BR_H, centered=False)
           .translate((x0, BR_Y0, T_FLOOR - 0.1)))
    if i == 1:
        tun = (cq.Workplane("XY").box(BR_TUN_W, BR_Y1 - BR_Y0 + 2, BR_TUN_H + 0.1, centered=False)
               .translate(((x0 + x1) / 2 - BR_TUN_W / 2, BR_Y0 - 1, T_FLOOR - 0.1)))
        blk = blk.cut(tun)
    box = box.union(blk)

# slotted post
post = (cq.Workplane("XY").box(UP_X1 - UP_X0, UP_Y1 - UP_Y0, UP_TOP - T_FLOOR + 0.1,
                               centered=False)
        .translate((UP_X0, UP_Y0, T_FLOOR - 0.1)))
ucx = (UP_X0 + UP_X1) / 2
slot = (cq.Workplane("XZ", origin=(0, UP_Y1 + 1, 0))
        .center(ucx, UP_TOP - UP_SLOT_D / 2 + UP_SLOT_W / 4 + 0.5)
        .slot2D(UP_SLOT_D + UP_SLOT_W / 2 + 1, UP_SLOT_W, 90)
        .extrude(UP_Y1 - UP_Y0 + 2))
post = post.cut(slot)
box = box.union(post)

# front panel
pn = (cq.Workplane("XZ", origin=(0, -BY / 2, 0))
      .center(0, (PN_Z0 + PN_Z1) / 2)
      .rect(PN_W, PN_Z1 - PN_Z0).extrude(PN_T)
      .edges("|Y").fillet(PN_R))
pn = pn.faces("<Y or >Y").edges().fillet(PN_EDGE)
pn_holes = (cq.Workplane("XZ", origin=(0, -BY / 2 + 1, 0))
            .pushPoints(PN_HOLES).circle(PN_HOLE_D / 2).extrude(PN_T + 2))
pn = pn.cut(pn_holes)
wx0, wx1, wz0, wz1 = PN_WIN
pn_win = (cq.Workplane("XZ", origin=(0, -BY / 2 + 1, 0))
          .center((wx0 + wx1) / 2, (wz0 + wz1) / 2)
          .rect(wx1 - wx0, wz1 - wz0).extrude(PN_T + 2))
pn = pn.cut(pn_win)
box = box.union(pn)
# the lower panel holes and part of the window continue through the front wall
wall_holes = (cq.Workplane("XZ", origin=(0, -BY / 2 + T_WALL + 1, 0))
              .pushPoints([p for p in PN_HOLES if p[1] < BH])
              .circle(PN_HOLE_D / 2).extrude(T_WALL + 2))
box = box.cut(wall_holes)
wwx0, wwx1, wwz0, wwz1 = WALL_WIN
wall_win = (cq.Workplane("XZ", origin=(0, -BY / 2 + T_WALL + 1, 0))
            .center((wwx0 + wwx1) / 2, (wwz0 + wwz1) / 2)
            .rect(wwx1 - wwx0, wwz1 - wwz0).extrude(T_WALL + 2))
box = box.cut(wall_win)

# ---------------- lid ----------------
lid = rrect(LX, LY, R_OUT, 0, LH)
lid = lid.faces(">Z").edges().fillet(L_FIL)
lid = lid.faces("<Z").shell(-L_T)
collar = (cq.Workplane("XY").workplane(offset=LH - L_T - L_COLLAR)
          .center(L_WIN_DX, L_WIN_DY)
          .rect(L_WIN_W + 2 * L_T, L_WIN_H + 2 * L_T).extrude(L_COLLAR + 0.05))
lid = lid.union(collar)
lid_win = (cq.Workplane("XY").workplane(offset=-1)
           .center(L_WIN_DX, L_WIN_DY).rect(L_WIN_W, L_WIN_H).extrude(LH + 2))
lid = lid.cut(lid_win)
lid_pts = corner_pts(LX, LY)
lid_h = (cq.Workplane("XY").workplane(offset=-1)
         .pushPoints(lid_pts).circle(L_HOLE_D / 2).extrude(LH + 2))
lid = lid.cut(lid_h)
lid = lid.translate((LID_CX, LID_CY, LID_Z0))

result = box.union(lid)

VIEW = {"azimuth": 45, "elevation": 26}
